import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BOX_W = 40.0        # box width  (X)
BOX_L = 76.0        # box length (Y)
BOX_H = 34.0        # box body height (Z), without lip
LIP_H = 4.5         # height of the lid lip on top
LIP_INSET = 2.2     # lip outer face inset from body outer face
WALL_TOP = 3.8      # wall thickness of the lip collar (outer body face -> cavity)
COLLAR_DEPTH = 7.1  # depth (from lip top) of the thick collar at the cavity mouth
WALL = 3.0          # wall thickness below the collar (+X, +Y and -Y walls)
WALL_NX = 3.8       # -X wall is flush with the collar all the way down
FLOOR_T = 2.5       # floor thickness
CORNER_R = 2.2      # vertical corner radius of the body
BOTTOM_R = 2.5      # bottom edge round
TOP_R = 0.8         # round on the body's top outer edge (shoulder)
LIP_R = 1.0         # lip corner radius

TUBE_OD = 33.4      # tube outer diameter
TUBE_ID = 28.8      # tube inner diameter
TUBE_ANGLE = 45.0   # tube angle below horizontal (towards +X)
TUBE_LEN = 91.0     # tube length from the box bottom +X edge to its end
TUBE_Y = -15.6      # tube axis offset along Y from box centre
TUBE_BACK = 20.0    # how far the solid tube reaches back into the box

# front (-Y) face features
SLOT_X, SLOT_Z, SLOT_W, SLOT_H = -9.5, 15.7, 3.6, 19.6
FHOLE_X, FHOLE_Z, FHOLE_D = 8.9, 17.3, 9.4
# back (+Y) face features
BHOLE_X, BHOLE_Z, BHOLE_D = -5.9, 19.3, 20.6
SHOLE_X, SHOLE_Z, SHOLE_D = 11.4, 10.0, 9.2
# wire hole from the cavity into the (blind) tube bore, parallel to the tube
WHOLE_Y, WHOLE_D = -23.4, 10.5


def tube_cylinder(radius, length, start, seam_spin=0.0):
    """Solid cylinder along the tube axis starting at `start`.

    Built along +Z (seam on +X), spun about its own axis to place the seam
    (0 = underside of the inclined tube, 180 = top), then tilted down by
    TUBE_ANGLE towards +X and moved into place.
    """
    c = cq.Solid.makeCylinder(radius, length, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_spin)
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90.0 + TUBE_ANGLE)
    c = c.translate(start)
    return cq.Workplane("XY").add(c)


# ---------------- box body ----------------
body = cq.Workplane("XY").rect(BOX_W, BOX_L).extrude(BOX_H)
# round the bottom edges, except the +X bottom edge where the tube sits
bottom_edges = [
    e for e in body.faces("<Z").edges().vals() if e.Center().x < BOX_W / 2 - 0.1
]
body = body.newObject(bottom_edges).fillet(BOTTOM_R)
body = body.edges("|Z").fillet(CORNER_R)
body = body.faces(">Z").edges().fillet(TOP_R)

lip = (
    cq.Workplane("XY", origin=(0, 0, BOX_H - 0.5))
    .rect(BOX_W - 2 * LIP_INSET, BOX_L - 2 * LIP_INSET)
    .extrude(LIP_H + 0.5)
    .edges("|Z").fillet(LIP_R)
)
box = body.union(lip)

# ---------------- tube (solid) ----------------
a = math.radians(TUBE_ANGLE)
tdir = cq.Vector(math.cos(a), 0, -math.sin(a))          # tube axis direction
corner = cq.Vector(BOX_W / 2, TUBE_Y, 0)                # axis meets bottom +X edge
t_start = corner - tdir * TUBE_BACK

tube = tube_cylinder(TUBE_OD / 2, TUBE_BACK + TUBE_LEN, t_start)
part = box.union(tube)

# ---------------- cavity ----------------
top_z = BOX_H + LIP_H
# mouth of the cavity (through the lip collar)
cav_upper = (
    cq.Workplane("XY", origin=(0, 0, top_z - COLLAR_DEPTH))
    .rect(BOX_W - 2 * WALL_TOP, BOX_L - 2 * WALL_TOP)
    .extrude(COLLAR_DEPTH + 1)
)
# main cavity below the collar (slightly undercut on +X, +Y and -Y)
low_x0 = -BOX_W / 2 + WALL_NX
low_x1 = BOX_W / 2 - WALL
cav_lower = (
    cq.Workplane("XY", origin=((low_x0 + low_x1) / 2, 0, FLOOR_T))
    .rect(low_x1 - low_x0, BOX_L - 2 * WALL)
    .extrude(top_z - COLLAR_DEPTH - FLOOR_T + 0.01)
)
part = part.cut(cav_upper).cut(cav_lower)

# ---------------- tube bore (blind, ends at the box corner plane) ----------------
bore = tube_cylinder(TUBE_ID / 2, TUBE_LEN + 1, corner, seam_spin=180.0)
part = part.cut(bore)

# wire hole connecting cavity and bore (parallel to the tube axis)
w_start = cq.Vector(BOX_W / 2, WHOLE_Y, 0) - tdir * 14.0
whole = tube_cylinder(WHOLE_D / 2, 17.0, w_start)
part = part.cut(whole)

# ---------------- holes in the end walls ----------------
y_front = -BOX_L / 2
y_back = BOX_L / 2
cut_len = WALL_TOP + 3

slot = (
    cq.Workplane("XZ", origin=(0, y_front + WALL_TOP + 1, 0))
    .center(SLOT_X, SLOT_Z)
    .rect(SLOT_W, SLOT_H)
    .extrude(cut_len)
    .edges("|Y").fillet(0.5)
)
fhole = (
    cq.Workplane("XZ", origin=(0, y_front + WALL_TOP + 1, 0))
    .center(FHOLE_X, FHOLE_Z)
    .circle(FHOLE_D / 2)
    .extrude(cut_len)
)
bhole = (
    cq.Workplane("XZ", origin=(0, y_back + 1, 0))
    .center(BHOLE_X, BHOLE_Z)
    .circle(BHOLE_D / 2)
    .extrude(cut_len)
)
shole = (
    cq.Workplane("XZ", origin=(0, y_back + 1, 0))
    .center(SHOLE_X, SHOLE_Z)
    .circle(SHOLE_D / 2)
    .extrude(cut_len)
)
part = part.cut(slot).cut(fhole).cut(bhole).cut(shole)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
